import math
import cadquery as cq

# ---- driving dimensions (mm) ----
S = 30.0            # width across flats
M = 15.0            # nut height
E = S / math.cos(math.radians(30))   # width across corners
CH_D = 30.2         # chamfer circle diameter on both faces (slightly > S)
CH_ANG = 45.0       # chamfer angle from the face (deg)
HOLE_D = 16.45      # bore (thread minor) diameter
CSK_D = 21.0        # countersink diameter at the faces
CSK_ANG = 90.0      # included countersink angle
PITCH = 1.5         # thread pitch (modelled as annular grooves)
N_GROOVES = 7       # number of thread grooves
TH_DEPTH = 0.8      # groove depth (radial)
TH_FLAT = 0.19      # flat at groove root (major diameter)
TH_SHIFT = 0.2      # axial offset of the groove pattern (thread phase)
SEAM_ANG = 45.0     # angular position of the bore revolve seam (cosmetic)
CSK_SEAM = -45.0    # angular position of the countersink seams (cosmetic)
GROOVE_SEAM = 45.0  # angular position of the groove revolve seams (cosmetic)

# hex prism, vertices on +/-X, flats facing +/-Y
body = cq.Workplane("XY").polygon(6, E).extrude(M)

# double-sided chamfer: intersect with a revolved "bicone" profile
r0 = CH_D / 2.0
big = E
dz = (big - r0) * math.tan(math.radians(CH_ANG))
cham = (
    cq.Workplane("XZ")
    .polyline([(0, 0), (r0, 0), (big, dz), (big, M - dz), (r0, M), (0, M)])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
body = body.intersect(cham)

# plain bore (thread minor diameter)
rh = HOLE_D / 2.0
rc = CSK_D / 2.0
t = math.tan(math.radians(CSK_ANG / 2.0))
cd = (rc - rh) / t          # countersink depth
eps = 0.5
bore = (
    cq.Workplane("XZ")
    .polyline([(0, -eps), (rh, -eps), (rh, M + eps), (0, M + eps)])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), SEAM_ANG)
)
body = body.cut(bore)

# 90-degree countersinks on both faces (cones, apex on the axis)
r_out = rc + eps * t
h_cone = r_out / t
csk_bot = (
    cq.Workplane("XZ")
    .polyline([(0, -eps), (r_out, -eps), (0, -eps + h_cone)])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), CSK_SEAM)
)
csk_top = csk_bot.mirror("XY", (0, 0, M / 2.0))
body = body.cut(csk_bot).cut(csk_top)

# thread represented by annular 60-degree grooves
half_w = TH_FLAT / 2.0 + TH_DEPTH * math.tan(math.radians(30))
z0 = M / 2.0 - (N_GROOVES - 1) / 2.0 * PITCH + TH_SHIFT
for k in range(N_GROOVES):
    zc = z0 + k * PITCH
    g = (
        cq.Workplane("XZ")
        .polyline([
            (rh - 0.2, zc - half_w - 0.2 * math.tan(math.radians(30))),
            (rh + TH_DEPTH, zc - TH_FLAT / 2.0),
            (rh + TH_DEPTH, zc + TH_FLAT / 2.0),
            (rh - 0.2, zc + half_w + 0.2 * math.tan(math.radians(30)))])
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .rotate((0, 0, 0), (0, 0, 1), GROOVE_SEAM)
    )
    body = body.cut(g)

result = body
